import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 116.0            # overall width (X)
HW = W / 2.0
Y_SIDE = 65.2        # length of the straight sides (front at y=0)
Y_APEX = 75.9        # depth at the centre of the curved back
H = 8.8              # height of the shell walls
R_ROLL = 8.6         # radius of the rounded bottom edges along the sides
T_WALL = 2.4         # outer wall thickness (incl. lip)
T_FLOOR = 2.0        # floor thickness (floor top at z = T_FLOOR)
R_COVE = 3.5         # cove between floor and curved back wall

LIP_W = 0.8          # mating lip width
LIP_H = 1.2          # mating lip height

NOTCH_HX = 36.0      # half width of the front (connector) notch
LEDGE_H = 2.8        # height of the ledge in the notch
LEDGE_D = 11.5       # depth of the ledge (y)
LEDGE_R = 1.35       # radius of the rounded ledge nose
FWALL_T = 1.5        # thickness of the inner front wall behind the ledge
FWALL_H = 7.4        # height of that inner front wall (PCB support level)
BLOCK_T = 1.5        # wall thickness of the corner blocks facing the notch

RIB_X = 50.85        # x position (centre) of the side channel ribs
RIB_T = 1.0
RIB_H = 7.4          # top of the channel ribs
CH_FLOOR = 5.0       # floor height of the side channels
BLK_FLOOR = 4.6      # floor of the pockets inside the front corner blocks

# side notch in the -X wall
SN_Y0, SN_Y1 = 37.5, 52.4
SN_X = 52.2          # wall moved in to x = -SN_X
SN_Z = 3.5           # floor of the side notch
# +X side: zone where the channel is filled flush with the rim (no lip)
PX_Y0, PX_Y1 = 39.3, 55.0

# underside
STRIP_D = 0.25       # central strip of the underside stands proud by this
LBL_HX = 31.0        # label recess half width
LBL_Y0 = 6.0         # label recess front edge
LBL_INSET = 6.0      # label recess inset from the curved back edge
LBL_R = 3.0          # label recess corner radius
LBL_D = 0.4          # label recess depth

# grip recess on the rolled edges near the front
GRIP_D = 0.5
GRIP_CY, GRIP_CZ, GRIP_R = 0.0, 15.2, 25.1

MARK_X = 33.9        # position of the small alignment marks / back step
GRIP_MARK_Y = 24.3   # small marks at the top of the side faces
BACK_PROUD = 0.3

# bosses
CONE_X, CONE_Y = 33.9, 64.2
CONE_RB, CONE_RT, CONE_TOP = 3.4, 2.55, 9.8
FB_X, FB_Y, FB_R, FB_TOP = 47.4, 8.7, 3.0, 7.6
CB_X, CB_Y, CB_R, CB_TOP = -8.6, 32.8, 3.3, 7.4

# shallow rectangular recess in the floor
PAD = (-45.7, -23.75, 17.1, 56.8)
PAD_D = 0.6

# arc of the back edge (through (+-HW, Y_SIDE) and (0, Y_APEX))
SAG = Y_APEX - Y_SIDE
R_BACK = (HW ** 2 + SAG ** 2) / (2 * SAG)
YC_BACK = Y_APEX - R_BACK


def back_y(x, off=0.0):
    """y of the back arc (offset inwards by off) at abscissa x."""
    r = R_BACK - off
    return YC_BACK + math.sqrt(r * r - x * x)


def outline(off=0.0, ext=0.0):
    """Top-view outline offset inwards by 'off' (front extended by ext)."""
    x = HW - off
    ys = back_y(x, off)
    return (
        cq.Workplane("XY")
        .moveTo(-x, off - ext)
        .lineTo(x, off - ext)
        .lineTo(x, ys)
        .threePointArc((0, Y_APEX - off), (-x, ys))
        .close()
    )


def region(x0, x1, y0, y1, z0, z1):
    x0, x1 = sorted((x0, x1))
    y0, y1 = sorted((y0, y1))
    return (
        cq.Workplane("XY")
        .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
        .translate((x0, y0, z0))
    )


def side_profile(d=0.0, zt=H):
    """XZ cross-section with rolled bottom edges; d insets sides and rolls."""
    xc = HW - R_ROLL
    w = (
        cq.Workplane("XZ")
        .moveTo(-(HW - d), zt)
        .lineTo(HW - d, zt)
        .lineTo(HW - d, R_ROLL)
        .radiusArc((xc, d), R_ROLL - d)
    )
    if d > 0:
        w = w.lineTo(xc, -1).lineTo(-xc, -1).lineTo(-xc, d)
    else:
        w = w.lineTo(-xc, 0)
    w = w.radiusArc((-(HW - d), R_ROLL), R_ROLL - d).close()
    return w.extrude(-90).translate((0, -5, 0))


# ---------------- outer body ----------------
plan = outline().extrude(H)
body = side_profile().intersect(plan)

# central strip of the underside (slightly proud)
body = body.union(
    outline().extrude(1.0 + STRIP_D).translate((0, 0, -STRIP_D))
    .intersect(region(-NOTCH_HX, NOTCH_HX, -1, 100, -1, 2))
)

# slightly proud centre band of the curved back face
body = body.union(
    outline(-BACK_PROUD).extrude(H)
    .cut(outline().extrude(H))
    .intersect(region(-MARK_X, MARK_X, 40, 100, -1, H + 1))
)

# front connector notch -> ledge
body = body.cut(region(-NOTCH_HX, NOTCH_HX, -1, LEDGE_D, LEDGE_H, H + 5))
# round nose of the ledge
body = body.edges(
    cq.selectors.BoxSelector((-NOTCH_HX + 0.1, -0.1, -STRIP_D - 0.1),
                             (NOTCH_HX - 0.1, 0.1, LEDGE_H + 0.1))
).fillet(LEDGE_R)

# label recess on the underside
lbl = (
    outline(LBL_INSET).extrude(1.0)
    .intersect(region(-LBL_HX, LBL_HX, LBL_Y0, 100, -1, 2))
    .edges("|Z").fillet(LBL_R)
    .translate((0, 0, -STRIP_D - 1.0 + LBL_D))
)
body = body.cut(lbl)

# grip recesses on the rolled side edges near the front
grip_zone = (
    cq.Workplane("YZ").workplane(offset=-HW - 5)
    .center(GRIP_CY, GRIP_CZ).circle(GRIP_R).extrude(W + 10)
    .intersect(region(-HW - 5, HW + 5, -5, 40, -5, R_ROLL - 0.5))
)
skin = side_profile().cut(side_profile(GRIP_D, H + 1))
body = body.cut(skin.intersect(grip_zone))

# small vertical marks at the top of the side faces (end of the grip zone)
for s in (-1, 1):
    body = body.cut(region(s * (HW + 1), s * (HW - 0.4), GRIP_MARK_Y - 0.3, GRIP_MARK_Y + 0.3,
                           H - 1.2, H + 1))

# small alignment marks on the ledge nose
for s in (-1, 1):
    body = body.cut(cq.Workplane("XY").workplane(offset=-2)
                    .center(s * MARK_X, 0).circle(0.45).extrude(10))

# ---------------- interior ----------------
# main cavity (with a cove along the curved back wall)
main_cav = (
    outline(T_WALL).extrude(H + 5 - T_FLOOR).translate((0, 0, T_FLOOR))
    .intersect(region(-(RIB_X - RIB_T / 2), RIB_X - RIB_T / 2,
                      LEDGE_D + FWALL_T, 100, 0, H + 10))
)
# cove ring: revolved quarter-round profile about the axis of the back arc
rw = R_BACK - T_WALL
cove_ring = (
    cq.Workplane("YZ", origin=(0, YC_BACK, 0))
    .moveTo(rw - R_COVE, T_FLOOR - 0.01)
    .lineTo(rw + 0.5, T_FLOOR - 0.01)
    .lineTo(rw + 0.5, T_FLOOR + R_COVE)
    .lineTo(rw, T_FLOOR + R_COVE)
    .radiusArc((rw - R_COVE, T_FLOOR - 0.01), R_COVE)
    .close()
    .revolve(50, (0, 0, 0), (0, 1, 0))
    .rotate((0, YC_BACK, 0), (0, YC_BACK, 1), -25)
)
main_cav = main_cav.cut(cove_ring)
body = body.cut(main_cav)

for s in (-1, 1):
    # side channel between outer wall and rib
    ch = (
        outline(T_WALL).extrude(H + 5)
        .intersect(region(s * (RIB_X + RIB_T / 2), s * (HW - T_WALL),
                          LEDGE_D, 100, CH_FLOOR, H + 10))
    )
    body = body.cut(ch)
    # rib top lower than the shell rim
    body = body.cut(
        outline(T_WALL).extrude(5).translate((0, 0, RIB_H))
        .intersect(region(s * (RIB_X - RIB_T / 2 - 0.01), s * (RIB_X + RIB_T / 2 + 0.01),
                          LEDGE_D, 100, 0, H + 10))
    )
    # pocket inside the front corner block
    body = body.cut(region(s * (NOTCH_HX + BLOCK_T), s * (HW - T_WALL - 0.5),
                           T_WALL, LEDGE_D - 0.5, BLK_FLOOR, H + 10))
    # low cross wall at the back of the block pocket, open behind the boss
    body = body.cut(region(s * (NOTCH_HX + BLOCK_T), s * (RIB_X + RIB_T / 2),
                           LEDGE_D - 0.6, LEDGE_D + FWALL_T + 0.1, FWALL_H, H + 10))
    body = body.cut(region(s * (FB_X - FB_R - 0.3), s * (RIB_X - RIB_T / 2),
                           LEDGE_D - 0.6, LEDGE_D + FWALL_T + 0.1, BLK_FLOOR, H + 10))
    # small U-notch in the top of that cross wall
    body = body.cut(cq.Workplane("XZ", origin=(0, LEDGE_D - 1.0, 0))
                    .center(s * (NOTCH_HX + BLOCK_T + 1.6), FWALL_H)
                    .circle(0.7).extrude(-(FWALL_T + 2.0)))
    # the channel rib runs on to the front wall inside the block
    body = body.union(region(s * (RIB_X - RIB_T / 2), s * (RIB_X + RIB_T / 2),
                             T_WALL - 0.01, LEDGE_D + 0.01, BLK_FLOOR - 0.5, RIB_H))
    # stiffening cross rib on the channel rib
    body = body.union(region(s * (RIB_X - RIB_T / 2 + 0.01), s * (RIB_X - RIB_T / 2 - 3.4),
                             38.0, 39.0, 1.0, RIB_H))
    # PCB retaining clip across the channel near the back
    clip_y = 59.5
    body = body.union(region(s * (RIB_X - RIB_T / 2), s * (HW - T_WALL + 0.01),
                             clip_y, clip_y + 1.8, CH_FLOOR - 0.5, 8.0))
    body = body.cut(region(s * (RIB_X + 0.8), s * (RIB_X + 2.2),
                           clip_y - 0.1, clip_y + 2.0, 5.5, 9.0))

# inner front wall top (lower than shell rim)
body = body.cut(region(-NOTCH_HX - 0.01, NOTCH_HX + 0.01, LEDGE_D - 0.1,
                       LEDGE_D + FWALL_T + 0.1, FWALL_H, H + 10))

# side notch in the -X wall
body = body.cut(region(-HW - 1, -SN_X, SN_Y0, SN_Y1, SN_Z, H + 10))
body = body.union(region(-SN_X, -(RIB_X + RIB_T / 2), SN_Y0, SN_Y1, CH_FLOOR - 0.5, H))
# short walls closing the channel at both ends of the side notch
for yy in (SN_Y0 - 1.2, SN_Y1):
    body = body.union(region(-(HW - T_WALL) - 0.01, -SN_X, yy, yy + 1.2, CH_FLOOR - 0.5, H))

# +X side: channel filled flush with the rim over a short length
body = body.union(
    outline(0.01).extrude(H - CH_FLOOR + 0.5).translate((0, 0, CH_FLOOR - 0.5))
    .intersect(region(RIB_X - RIB_T / 2, HW, PX_Y0, PX_Y1, 0, H))
    .intersect(side_profile(0.01))
)

# ---------------- mating lip ----------------
lip = (
    outline(T_WALL - LIP_W).extrude(LIP_H)
    .cut(outline(T_WALL).extrude(LIP_H))
    .translate((0, 0, H))
)
lip = lip.cut(region(-NOTCH_HX, NOTCH_HX, -1, LEDGE_D + 5, H - 1, H + 5))
# no lip along the side-notch zone
lip = lip.cut(region(-HW - 1, -HW + 4, SN_Y0 - 0.01, SN_Y1 + 0.01, H - 1, H + 5))
lip = lip.cut(region(HW + 1, HW - 4, PX_Y0, PX_Y1, H - 1, H + 5))
lip = lip.cut(region(HW + 1, HW - 4, 54.7, 55.8, H - 1, H + 5))
# small gaps in the lip on the curved back wall (aligned with the marks)
for s in (-1, 1):
    lip = lip.cut(region(s * MARK_X - 0.5, s * MARK_X + 0.5, 50, 100, H - 1, H + 5))
# lip along the short walls closing the side notch
for yy in (SN_Y0 - 1.2, SN_Y1 + 0.3):
    lip = lip.union(region(-(HW - T_WALL), -SN_X, yy, yy + LIP_W, H, H + LIP_H))
# lip along the walls of the blocks facing the notch
for s in (-1, 1):
    lip = lip.union(region(s * (NOTCH_HX + BLOCK_T - LIP_W), s * (NOTCH_HX + BLOCK_T),
                           T_WALL - LIP_W, LEDGE_D, H, H + LIP_H))
body = body.union(lip)

# ---------------- bosses ----------------
for s in (-1, 1):
    cone = cq.Solid.makeCone(CONE_RB, CONE_RT, CONE_TOP - 1.0,
                             cq.Vector(s * CONE_X, CONE_Y, 1.0), cq.Vector(0, 0, 1))
    body = body.union(cq.Workplane().add(cone))
    body = body.cut(cq.Workplane("XY").workplane(offset=3.0)
                    .center(s * CONE_X, CONE_Y).circle(0.65).extrude(10))

    fb = cq.Solid.makeCone(FB_R + 0.3, FB_R, FB_TOP - 2.5,
                           cq.Vector(s * FB_X, FB_Y, 2.5), cq.Vector(0, 0, 1))
    body = body.union(cq.Workplane().add(fb))
    body = body.cut(cq.Workplane("XY").workplane(offset=3.2)
                    .center(s * FB_X, FB_Y).circle(1.0).extrude(10))
    body = body.cut(cq.Workplane().add(
        cq.Solid.makeCone(1.0, 1.4, 0.4, cq.Vector(s * FB_X, FB_Y, FB_TOP - 0.4), cq.Vector(0, 0, 1))))

cb = cq.Workplane("XY").workplane(offset=1.0).center(CB_X, CB_Y).circle(CB_R).extrude(CB_TOP - 1.0)
body = body.union(cb)

# shallow rectangular recess in the floor
body = body.cut(region(PAD[0], PAD[1], PAD[2], PAD[3], T_FLOOR - PAD_D, T_FLOOR + 1.0))

result = body
